import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
rod_d = 10.0          # rod / hub diameter
total_len = 80.0      # tip of rounded rod to back face of fins
fin_len = 29.0        # axial length of the fin cross (along +Y)
fin_span = 25.0       # tip-to-tip span of the cross (X and Z)
fin_t = 4.2           # fin plate thickness
fin_r = 8.2           # corner radius at the front (rod side) of each fin
seam_angle = 160.0    # rotate the revolved rod so its seam sits on a hidden side

rod_r = rod_d / 2.0
half = fin_span / 2.0
rod_len = total_len - fin_len   # rod ahead of the fins, including the round tip

# ---------------- rod + hub about the Y axis ----------------
# fin cross occupies 0 <= y <= fin_len, the rod points to -Y with a hemispherical tip
y_tip = -rod_len
y_c = y_tip + rod_r                      # centre of the hemispherical tip
c45 = math.cos(math.radians(45))
shaft = (
    cq.Workplane("XZ", origin=(0, fin_len, 0))
    .circle(rod_r)
    .extrude(fin_len - y_c)              # XZ normal is -Y: runs from the back face to the tip centre
)
tip = cq.Workplane("XY").sphere(rod_r).translate((0, y_c, 0))
rod = shaft.union(tip).rotate((0, 0, 0), (0, 1, 0), seam_angle)

# ---------------- fin plate profile (rounded front corners) ----------------
k = fin_r * (1 - c45)


def fin_plate(wp):
    # local coords: a = across the span, b = axial (+Y); extruded symmetrically
    return (
        wp.moveTo(-half, fin_len)
        .lineTo(half, fin_len)
        .lineTo(half, fin_r)
        .threePointArc((half - k, k), (half - fin_r, 0))
        .lineTo(-half + fin_r, 0)
        .threePointArc((-half + k, k), (-half, fin_r))
        .close()
        .extrude(fin_t / 2.0, both=True)
    )


# horizontal fin: lies in the XY plane, thickness along Z
fin_h = fin_plate(cq.Workplane("XY"))

# vertical fin: lies in the YZ plane, thickness along X (local a = Z, local b = Y)
fin_v = fin_plate(cq.Workplane(cq.Plane(origin=(0, 0, 0), xDir=(0, 0, 1), normal=(-1, 0, 0))))

result = rod.union(fin_h).union(fin_v).clean()

VIEW = {"azimuth": 45, "elevation": 26}
